import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 130.0          # plate length (X)
W = 50.0           # plate depth (Y)
T = 5.5            # plate thickness (rim top at z = T)
R_CORNER = 8.0     # plan corner radius
EDGE_R = 0.5       # outer edge round

YB = W / 2         # back edge y

# rail (dovetail slide along the back edge)
RAIL_H = 4.0                 # height above rim
RAIL_D = 9.1                 # depth of plain rail (from back edge)
DOVE_D = 10.65               # depth of dovetail top edge (from back edge)
DOVE_X = 50.5                # half length of dovetail top edge
DOVE_S = 3.1                 # length of S-transition at each end
DOVE_END_X = 50.5            # undercut ends here at its top edge ...
DOVE_END_K = 1.8             # ... and skews inward this much per mm of undercut
DOVE_ANG = 20.0              # dovetail undercut angle from vertical
RAIL_LIP = 0.35              # chamfer on rail top front edge

# pocket (3.1 deep recess inside the rim)
REC_X0, REC_X1 = -50.7, 50.6
REC_Y0 = -19.0
REC_DEPTH = 3.1
REC_UNDERCUT = 48.0          # deg, -X end wall undercut

# holes
HOLE_X = 50.5
HOLE_Y = YB - 6.9
HOLE_D = 3.5
HOLE_CH = 0.45
SMALL_D = 3.3
SMALL_CH = 0.4
TRIO_X = -56.4
TRIO_MID_DX = 1.3
TRIO_Y = [2.75, -2.75, -8.2]
RIGHT_HOLE = (55.4, -2.75)
BLIND_DEPTH = 2.3

# bullet shaped through opening
OP_X0, OP_X1 = -50.7, -1.1
OP_Y_TOP, OP_Y_BOT = 8.1, -13.1
OP_Y_TOP_END, OP_Y_BOT_END = 5.6, -10.6
OP_TAPER = 17.0
OP_LAND = 0.4                # straight wall below pocket floor
OP_RELIEF = 50.0             # deg undercut relief below the land

# raised guide block
BLK_X0, BLK_X1 = -3.7, 20.3
BLK_YC = 4.5
BLK_TOP_Z = T + 1.3
BLK_TOP_HW = 3.1             # half width of top flat
BLK_BASE_HW = BLK_TOP_HW + (BLK_TOP_Z - (T - REC_DEPTH))   # 45 deg flanks down to the floor
BLK_NOSE_CH = 2.0            # nose corner bevel
BLK_END_TOP_X = 16.7         # top flat ends here (inclined nose face)
PIN_D = 2.6
PIN_Z = T - 0.6

# scoop (countersink-like cone) cut into the block's -X end
SC_Y = 1.4                   # cone axis position
SC_Z = T + 0.3
SC_APEX_X = 13.6
SC_HALF_ANG = 21.3
BLK_DIAG = ((-3.7, 8.1), (2.7, 11.95))   # diagonal trim of the block's -X/+Y corner

# underside lens dimple
LENS_X = (3.0, 19.0)
LENS_Y = 4.2
LENS_W = 3.2
LENS_R = 4.0
LENS_DEPTH = 0.45

floor_z = T - REC_DEPTH
z_top = T + RAIL_H

# ---------------- base plate ----------------
base = (cq.Workplane("XY").rect(L, W).extrude(T)
        .edges("|Z").fillet(R_CORNER))
base = base.edges(">Z or <Z").fillet(EDGE_R)

# ---------------- pocket (undercut -X wall) ----------------
tan_u = math.tan(math.radians(REC_UNDERCUT))
x_u_floor = REC_X0 - REC_DEPTH * tan_u
x_u_hi = REC_X0 + 1.0 * tan_u
pk_y1 = YB - RAIL_D
pocket = (cq.Workplane("XZ", origin=(0, pk_y1, 0))
          .polyline([(x_u_floor, floor_z), (REC_X1, floor_z), (REC_X1, T + 1.0),
                     (x_u_hi, T + 1.0)]).close()
          .extrude(pk_y1 - REC_Y0))
body = base.cut(pocket)

# ---------------- rail ----------------
outline = (cq.Workplane("XY").workplane(offset=T - 0.5).rect(L, W)
           .extrude(RAIL_H + 0.5).edges("|Z").fillet(R_CORNER))
rail_box = (cq.Workplane("XY").center(0, YB - RAIL_D / 2)
            .rect(L + 2, RAIL_D).extrude(20))
rail = outline.intersect(rail_box)
rail = rail.edges(">Z").edges(">Y or <X or >X").fillet(EDGE_R)
body = body.union(rail)

# dovetail middle section with S-shaped ends (plan), vertical first
y_plain = YB - RAIL_D
y_dove = YB - DOVE_D
z_und = z_top - RAIL_LIP     # undercut starts just below the lip chamfer
y_under = y_dove + (z_und - floor_z) * math.tan(math.radians(DOVE_ANG))
xs = DOVE_X + DOVE_S
mid_plan = (cq.Workplane("XY").workplane(offset=floor_z)
            .moveTo(-xs, y_plain)
            .spline([(-DOVE_X, y_dove)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
            .lineTo(DOVE_X, y_dove)
            .spline([(xs, y_plain)], tangents=[(1, 0), (1, 0)], includeCurrent=True)
            .lineTo(xs, y_plain + 4)
            .lineTo(-xs, y_plain + 4)
            .close()
            .extrude(z_top - floor_z))
# below the rim level the dovetail only stands inside the pocket
mid_keep = (cq.Workplane("XY").center((REC_X0 + REC_X1) / 2, 0).rect(REC_X1 - REC_X0, W + 2)
            .extrude(T).union(cq.Workplane("XY").workplane(offset=T).rect(L + 2, W + 2).extrude(10)))
body = body.union(mid_plan.intersect(mid_keep))

# small lip chamfer along the rail's top front edge (before undercutting)
body = (body.edges(cq.selectors.BoxSelector((-L, y_dove - 0.2, z_top - 0.05),
                                            (L, y_plain + 0.2, z_top + 0.05)))
        .chamfer(RAIL_LIP))

# undercut wedge (front face leans back toward the floor), ends tapered
wedge_yz = (cq.Workplane("YZ", origin=(-xs - 2, 0, 0))
            .polyline([(y_under, floor_z), (y_dove, z_und),
                       (y_dove - 3, z_und), (y_dove - 3, floor_z)]).close()
            .extrude(2 * xs + 4))
# ends of the undercut: vertical planes skewed in plan, so the undercut reaches
# DOVE_END_X at its top edge and stops DOVE_END_K mm further in per mm of depth
y_far = y_under + 1.0
wedge_xz = (cq.Workplane("XY").workplane(offset=floor_z - 1)
            .polyline([(-DOVE_END_X, y_dove - 10), (DOVE_END_X, y_dove - 10), (DOVE_END_X, y_dove),
                       (DOVE_END_X - (y_far - y_dove) * DOVE_END_K, y_far),
                       (-DOVE_END_X + (y_far - y_dove) * DOVE_END_K, y_far), (-DOVE_END_X, y_dove)]).close()
            .extrude(z_top - floor_z + 3))
wedge = wedge_yz.intersect(wedge_xz)
body = body.cut(wedge)

# ---------------- through opening ----------------
def _ogive_mid(x0, y0, x1, y1):
    # point at mid-x on the circle through (x0,y0) tangent to horizontal at (x1,y1)
    dy = y1 - y0
    R = (OP_TAPER ** 2 + dy ** 2) / (2 * abs(dy))
    yc = y1 - math.copysign(R, dy)
    xm = (x0 + x1) / 2
    ym = yc + math.copysign(math.sqrt(R ** 2 - (xm - x1) ** 2), dy)
    return (xm, ym)


def opening_outline(wp):
    xm = OP_X0 + OP_TAPER
    return (wp.moveTo(OP_X0, OP_Y_BOT_END)
            .lineTo(OP_X0, OP_Y_TOP_END)
            .threePointArc(_ogive_mid(OP_X0, OP_Y_TOP_END, xm, OP_Y_TOP), (xm, OP_Y_TOP))
            .lineTo(OP_X1, OP_Y_TOP)
            .lineTo(OP_X1, OP_Y_BOT)
            .lineTo(xm, OP_Y_BOT)
            .threePointArc(_ogive_mid(OP_X0, OP_Y_BOT_END, xm, OP_Y_BOT), (OP_X0, OP_Y_BOT_END))
            .close())

op_main = opening_outline(cq.Workplane("XY").workplane(offset=-1)).extrude(T + 3)
body = body.cut(op_main)
z_relief = floor_z - OP_LAND
op_relief = (opening_outline(cq.Workplane("XY").workplane(offset=z_relief))
             .extrude(-(z_relief + 0.5), taper=-OP_RELIEF))
relief_clip = (cq.Workplane("XY").workplane(offset=-1)
               .center((REC_X0 - 4 + OP_X1 - 1.5) / 2, (OP_Y_TOP + 4 + OP_Y_BOT - 4) / 2)
               .rect(OP_X1 - 1.5 - (REC_X0 - 4), OP_Y_TOP - OP_Y_BOT + 8).extrude(T))
body = body.cut(op_relief.intersect(relief_clip))

# ---------------- guide block ----------------
yc = BLK_YC
blk = (cq.Workplane("YZ", origin=(BLK_X0, 0, 0))
       .polyline([(yc - BLK_BASE_HW, floor_z), (yc + BLK_BASE_HW, floor_z),
                  (yc + BLK_TOP_HW, BLK_TOP_Z), (yc - BLK_TOP_HW, BLK_TOP_Z)]).close()
       .extrude(BLK_X1 - BLK_X0))
# nose: inclined end face, then bevel the two edges between end face and flanks
nose = (cq.Workplane("XZ", origin=(0, yc + 10, 0))
        .polyline([(BLK_END_TOP_X, BLK_TOP_Z + 0.01), (BLK_X1 + 5, BLK_TOP_Z + 0.01),
                   (BLK_X1 + 5, floor_z - 0.01), (BLK_X1, floor_z - 0.01)]).close()
        .extrude(20))
blk = blk.cut(nose)
n_end = cq.Vector(BLK_TOP_Z - floor_z, 0, BLK_X1 - BLK_END_TOP_X).normalized()
for side in (-1, 1):
    p_top = cq.Vector(BLK_END_TOP_X, yc + side * BLK_TOP_HW, BLK_TOP_Z)
    p_bot = cq.Vector(BLK_X1, yc + side * BLK_BASE_HW, floor_z)
    e_dir = (p_bot - p_top).normalized()
    in_end = n_end.cross(e_dir).normalized()
    if in_end.y * side > 0:
        in_end = in_end * -1
    q1 = p_top + in_end * BLK_NOSE_CH
    q2 = p_top + cq.Vector(-BLK_NOSE_CH, 0, 0)            # back along the flank
    n = (q2 - q1).cross(e_dir).normalized()
    if n.dot(cq.Vector(1, 0, 0)) < 0:
        n = n * -1
    pl = cq.Plane(origin=q1, xDir=e_dir, normal=n)
    blk = blk.cut(cq.Workplane(pl).rect(60, 60).extrude(20))
# diagonal trim of the -X/+Y corner (plan view)
(dx0, dy0), (dx1, dy1) = BLK_DIAG
ux, uy = dx1 - dx0, dy1 - dy0
trim = (cq.Workplane("XY").workplane(offset=floor_z - 1)
        .polyline([(dx0 - 3 * ux, dy0 - 3 * uy), (dx1 + 3 * ux, dy1 + 3 * uy),
                   (dx0 - 3 * ux - 20, dy1 + 3 * uy + 5)]).close()
        .extrude(5))
blk = blk.cut(trim)
# trim block where it overlaps the opening
blk = blk.cut(op_main)
body = body.union(blk)

# scoop: cone (axis along X, apex toward +X) cut into the block's -X end
cone_h = SC_APEX_X - (BLK_X0 - 2.0)
r_base = cone_h * math.tan(math.radians(SC_HALF_ANG))
cone = cq.Solid.makeCone(r_base, 0.0, cone_h,
                         pnt=cq.Vector(BLK_X0 - 2.0, SC_Y, SC_Z), dir=cq.Vector(1, 0, 0))
scoop_clip = (cq.Workplane("XY").workplane(offset=-1).center((BLK_X0 + BLK_X1) / 2, 0)
              .rect(BLK_X1 - BLK_X0, 2 * (OP_Y_TOP + 3.5)).extrude(BLK_TOP_Z + 2))
body = body.cut(cq.Workplane("XY").add(cone).intersect(scoop_clip))

# pin hole in the block nose
pin = (cq.Workplane("YZ", origin=(BLK_X1 - 8, 0, 0))
       .center(yc, PIN_Z).circle(PIN_D / 2).extrude(12))
body = body.cut(pin)

# shallow lens-shaped dimple on the underside (below the block)
lx0, lx1 = LENS_X
lens_plan = (cq.Workplane("XY").workplane(offset=-1)
             .moveTo(lx0, LENS_Y)
             .threePointArc(((lx0 + lx1) / 2, LENS_Y + LENS_W / 2), (lx1, LENS_Y))
             .threePointArc(((lx0 + lx1) / 2, LENS_Y - LENS_W / 2), (lx0, LENS_Y))
             .close().extrude(2))
lens_cyl = cq.Workplane("XY").add(
    cq.Solid.makeCylinder(LENS_R, lx1 - lx0 + 2,
                          pnt=cq.Vector(lx0 - 1, LENS_Y, LENS_R - LENS_DEPTH),
                          dir=cq.Vector(1, 0, 0)))
body = body.cut(lens_plan.intersect(lens_cyl))

# ---------------- holes ----------------
def hole(x, y, d, ch, top_z, depth=None):
    global body
    zb = -1 if depth is None else top_z - depth
    h = (cq.Workplane("XY").workplane(offset=zb).center(x, y)
         .circle(d / 2).extrude(top_z - zb + 1))
    c = cq.Solid.makeCone(d / 2 + ch + 1.0, d / 2 - 0.01, ch + 1.0,
                          pnt=cq.Vector(x, y, top_z + 1.0), dir=cq.Vector(0, 0, -1))
    body = body.cut(h).cut(cq.Workplane("XY").add(c))


for sx in (-1, 1):
    hole(sx * HOLE_X, HOLE_Y, HOLE_D, HOLE_CH, z_top)
for i, y in enumerate(TRIO_Y):
    if i == 1:
        hole(TRIO_X + TRIO_MID_DX, y, SMALL_D, SMALL_CH, T, depth=BLIND_DEPTH)
    else:
        hole(TRIO_X, y, SMALL_D, SMALL_CH, T)
hole(RIGHT_HOLE[0], RIGHT_HOLE[1], SMALL_D, SMALL_CH, T, depth=BLIND_DEPTH)

result = body
